import cadquery as cq

# Open-backed terminal/junction box housing with curved mounting flanges,
# a cable-entry boss on the front and a ribbed/windowed top plate.

# ---------------- driving dimensions (mm) ----------------
D = 100.0           # body depth (Y); closed front face at -D/2, open back at +D/2
W = 70.7            # body width between outer wall faces (X)
H = 43.0            # height to the flange top faces (Z)
PANEL_H = 0.35      # raised central panel on top
PANEL_X = 32.6      # half width of the raised panel
PANEL_INSET = 2.7   # inset of the raised panel from the front face
WF = 89.4           # overall flange width (X) at mid depth
R_ARC = 250.0       # plan radius of the flange outer edges
R_CORNER = 8.0      # plan corner radius of the flanges
TF = 3.4            # flange thickness
T_TOP = 2.6         # top plate thickness over the cavity
T_BOT = 2.6         # floor thickness
T_WALL = 2.0        # side and front wall thickness
R_FLANGE_FIL = 2.0  # fillet between flanges and side walls
R_BOT_EDGE = 1.4    # rounding of the bottom outer edges
R_TOP_EDGE = 1.2    # rounding of the top outer edges

# cable entry boss on the front face
BOSS_D = 25.7
BOSS_HOLE = 19.2
BOSS_LEN = 4.9
BOSS_X = -16.4
BOSS_Z = 28.6
BOSS_FIL = 1.5

# mounting slots in the flanges (top and bottom, two per side)
SLOT_W = 4.1
SLOT_L = 14.5
SLOT_X0 = W / 2      # inner edge of slot: flush with the wall, cuts away the fillet
SLOT_YC = 21.7
COLLAR_T = 0.6      # thin rim around the slots on the underside
COLLAR_H = 0.85

# windows / pockets in the top plate
OPEN_X = 29.8                  # windows reach |x| = OPEN_X
BAR_X0, BAR_X1 = 10.1, 12.5    # longitudinal bar between the left and right windows
BIG_Y0, BIG_Y1 = -28.4, 31.2   # main window and narrow right recess
FRONT_Y0, FRONT_Y1 = -44.8, -35.1
NOTCH_Y0 = 38.3                # rear notch (open to the rear edge)
NOTCH_Y2 = 47.7                # the notch widens to the panel width near the rear edge
OPEN_R = 3.0
LEDGE_X = 17.2                 # free edge of the ledge inside the narrow right window
LEDGE_DEPTH = 2.0              # ledge depth below the top face
LEDGE_T = 1.5                  # ledge thickness
SHELF_GAP = 0.9                # slit between the ledge and the lower shelf
SHELF_T = 1.5                  # lower shelf thickness
SHELF_STEP_X = 26.4            # step in the lower shelf
STEP_NOTCH_X = 27.7            # notch in the shelf step along the window edge
STEP_NOTCH_Y1 = 11.4
FRONT_BEAM_Z = 35.3            # underside of the thickened front part of the top plate
FRONT_RECESS = 2.6             # depth of the front pockets
FRONT_INNER = 5.0              # depth of the inner (deeper) front pockets
FL_IN = (-27.4, 8.8, -42.7, -36.1)    # inner pocket, front left
FR_IN = (17.0, 28.0, -42.7, -36.1)    # inner pocket, front right

# interior details
FLOOR_HOLE_D = 3.7
FLOOR_HOLE_Y = 47.7
FLOOR_HOLE_DEPTH = 1.3
POCKET_X0, POCKET_X1 = -27.4, 8.8
POCKET_Y0, POCKET_Y1 = -42.7, 36.0
POCKET_DEPTH = 0.8
PAD_Y0, PAD_Y1 = 40.4, 47.8    # thickening pads on the inside of the side walls near the back
PAD_T = 1.5
PAD_TOP = 22.0

VIEW = {"azimuth": 45, "elevation": 26}

H_TOP = H + PANEL_H            # highest point of the top face


def rrect(x0, x1, y0, y1, r, z0, h):
    """Rounded-corner rectangular prism from z0 to z0+h."""
    w = cq.Workplane("XY").workplane(offset=z0).center((x0 + x1) / 2, (y0 + y1) / 2)
    w = w.rect(abs(x1 - x0), abs(y1 - y0)).extrude(h)
    if r > 0:
        w = w.edges("|Z").fillet(r)
    return w


def flange_plan(z0, h):
    """Plan shape: lens of two big arcs clipped to the body depth, corners rounded."""
    xc = R_ARC - WF / 2.0
    c1 = cq.Workplane("XY").workplane(offset=z0).center(xc, 0).circle(R_ARC).extrude(h)
    c2 = cq.Workplane("XY").workplane(offset=z0).center(-xc, 0).circle(R_ARC).extrude(h)
    box = cq.Workplane("XY").workplane(offset=z0).rect(WF + 10, D).extrude(h)
    lens = c1.intersect(c2).intersect(box)
    return lens.edges("|Z").fillet(R_CORNER)


# ---------------- outer body ----------------
# I-beam cross-section (side walls + top/bottom flanges), concave corners filleted
ibeam = (
    cq.Workplane("XY").rect(WF + 10, D).extrude(TF)
    .union(cq.Workplane("XY").rect(W, D).extrude(H))
    .union(cq.Workplane("XY").workplane(offset=H - TF).rect(WF + 10, D).extrude(TF))
)
ibeam = ibeam.edges("|Y").edges(
    cq.selectors.BoxSelector((-W / 2 - 0.1, -D, TF - 0.1), (W / 2 + 0.1, D, H - TF + 0.1))
).fillet(R_FLANGE_FIL)

# clip with the plan prism (its corner radius also rounds the vertical body corners)
body = ibeam.intersect(flange_plan(0, H))

# rounded outer edges along the top and bottom perimeter
try:
    body = body.faces(">Z").edges().fillet(R_TOP_EDGE)
except Exception:
    pass
try:
    body = body.faces("<Z").edges().fillet(R_BOT_EDGE)
except Exception:
    pass

# slightly raised central panel on the top face (inset from the front and side faces)
panel = (
    cq.Workplane("XY").workplane(offset=H - 0.01)
    .center(0, PANEL_INSET / 2)
    .rect(2 * PANEL_X, D - PANEL_INSET)
    .extrude(PANEL_H + 0.01)
    .edges("|Z").edges(cq.selectors.BoxSelector((-W, -D, 0), (W, 0, H + 1)))
    .fillet(2.0)
)
body = body.union(panel)

# ---------------- cable entry boss on the front face ----------------
boss = (
    cq.Workplane("XZ", origin=(0, -D / 2 + 1.0, 0))
    .center(BOSS_X, BOSS_Z)
    .circle(BOSS_D / 2)
    .extrude(BOSS_LEN + 1.0)
)
body = body.union(boss)
try:
    body = body.edges(
        cq.selectors.BoxSelector(
            (BOSS_X - BOSS_D / 2 - 0.2, -D / 2 - 0.2, BOSS_Z - BOSS_D / 2 - 0.2),
            (BOSS_X + BOSS_D / 2 + 0.2, -D / 2 + 0.2, BOSS_Z + BOSS_D / 2 + 0.2),
        )
    ).fillet(BOSS_FIL)
except Exception:
    pass

# ---------------- hollow interior, open at the back ----------------
cav = (
    cq.Workplane("XY")
    .workplane(offset=T_BOT)
    .center(0, T_WALL / 2 + 1)
    .rect(W - 2 * T_WALL, D - T_WALL + 2)
    .extrude(H - T_BOT - T_TOP)
)
body = body.cut(cav)

# thickened front part of the top plate (carries the front pockets)
x_in = W / 2 - T_WALL
front_beam = rrect(-x_in - 0.1, x_in + 0.1, -D / 2 + T_WALL - 0.1, BIG_Y0, 0, FRONT_BEAM_Z, H - T_TOP - FRONT_BEAM_Z + 0.1)
body = body.union(front_beam)

# ledge under the narrow right window (slightly thicker than the remaining plate)
ledge = rrect(BAR_X0, LEDGE_X, BIG_Y0 - 1.0, BIG_Y1 + 1.0, 0, H_TOP - LEDGE_DEPTH - LEDGE_T, LEDGE_T)
body = body.union(ledge)

# bore through boss and front wall
hole = (
    cq.Workplane("XZ", origin=(0, -D / 2 + T_WALL + 0.3, 0))
    .center(BOSS_X, BOSS_Z)
    .circle(BOSS_HOLE / 2)
    .extrude(BOSS_LEN + T_WALL + 5)
)
body = body.cut(hole)

# ---------------- windows, pockets and notch in the top plate ----------------
zc = H - TF - 1
hc = TF + PANEL_H + 2
cuts = [
    # main window (through)
    rrect(-OPEN_X, BAR_X0, BIG_Y0, BIG_Y1, OPEN_R, zc, hc),
    # narrow right window: shallow ledge along the bar, through opening beyond it
    rrect(BAR_X1, OPEN_X, BIG_Y0, BIG_Y1, OPEN_R, H_TOP - LEDGE_DEPTH, LEDGE_DEPTH + 1),
    rrect(LEDGE_X, OPEN_X, BIG_Y0, BIG_Y1, 1.5, zc - 2, hc + 2),
    # front pockets (stepped, blind)
    rrect(-OPEN_X, BAR_X0, FRONT_Y0, FRONT_Y1, 2.0, H_TOP - FRONT_RECESS, FRONT_RECESS + 1),
    rrect(BAR_X1, OPEN_X, FRONT_Y0, FRONT_Y1, 2.0, H_TOP - FRONT_RECESS, FRONT_RECESS + 1),
    rrect(FL_IN[0], FL_IN[1], FL_IN[2], FL_IN[3], 2.0, H_TOP - FRONT_INNER, FRONT_INNER + 1),
    rrect(FR_IN[0], FR_IN[1], FR_IN[2], FR_IN[3], 2.0, H_TOP - FRONT_INNER, FRONT_INNER + 1),
    # rear notch, open to the back edge
    rrect(-OPEN_X, OPEN_X, NOTCH_Y0, D / 2 + 5, 2.0, zc, hc),
    rrect(-PANEL_X, PANEL_X, NOTCH_Y2, D / 2 + 5, 0.6, zc, hc),
]
for c in cuts:
    body = body.cut(c)

# lower shelf under the through part of the narrow right window (leaves a slit below the ledge)
z_shelf_top = H_TOP - LEDGE_DEPTH - LEDGE_T - SHELF_GAP
x_wall_in = W / 2 - T_WALL + 0.1
lower_shelf = rrect(LEDGE_X, x_wall_in, BIG_Y0 - 1.0, BIG_Y1 + 1.0, 0, z_shelf_top - SHELF_T, SHELF_T)
shelf_step = rrect(SHELF_STEP_X, x_wall_in, BIG_Y0 - 1.0, BIG_Y1 + 1.0, 0, z_shelf_top - 0.1, H - T_TOP - z_shelf_top + 0.2)
body = body.union(lower_shelf).union(shelf_step)
body = body.cut(rrect(STEP_NOTCH_X, OPEN_X, BIG_Y0 - 0.5, STEP_NOTCH_Y1, 0.3, z_shelf_top, H_TOP - z_shelf_top + 1))

# ---------------- thin rims around the slots on the underside ----------------
for sx in (-1, 1):
    for sy in (-1, 1):
        xa = sx * (SLOT_X0 - COLLAR_T)
        xb = sx * (SLOT_X0 + SLOT_W + COLLAR_T)
        rim = rrect(min(xa, xb), max(xa, xb), sy * SLOT_YC - SLOT_L / 2 - COLLAR_T, sy * SLOT_YC + SLOT_L / 2 + COLLAR_T,
                    0.8 + COLLAR_T, -COLLAR_H, COLLAR_H + 0.3)
        body = body.union(rim)

# ---------------- mounting slots (cut through flange and wall fillet) ----------------
for sx in (-1, 1):
    for sy in (-1, 1):
        x0 = sx * SLOT_X0
        x1 = sx * (SLOT_X0 + SLOT_W)
        for z0, h in ((-1.0, TF + R_FLANGE_FIL + 1.0), (H - TF - R_FLANGE_FIL, TF + R_FLANGE_FIL + 1.0)):
            s = rrect(min(x0, x1), max(x0, x1), sy * SLOT_YC - SLOT_L / 2, sy * SLOT_YC + SLOT_L / 2, 0.8, z0, h)
            body = body.cut(s)

# ---------------- interior details ----------------
# shallow pocket in the floor
body = body.cut(rrect(POCKET_X0, POCKET_X1, POCKET_Y0, POCKET_Y1, 3.0, T_BOT - POCKET_DEPTH, 2.0))
# small blind hole in the floor near the open back
body = body.cut(
    cq.Workplane("XY").workplane(offset=T_BOT - FLOOR_HOLE_DEPTH).center(0, FLOOR_HOLE_Y)
    .circle(FLOOR_HOLE_D / 2).extrude(FLOOR_HOLE_DEPTH + 1)
)
# thickening pads on the inside of both side walls near the open back
for sx in (-1, 1):
    xa = sx * (W / 2 - T_WALL + 0.1)
    xb = sx * (W / 2 - T_WALL - PAD_T)
    pad = rrect(min(xa, xb), max(xa, xb), PAD_Y0, PAD_Y1, 0, T_BOT - 0.1, PAD_TOP - T_BOT + 0.1)
    body = body.union(pad)

result = body
